import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Cloverleaf (4-lobe) wire antenna on a two-piece 12-sided hub.
# Each lobe is a closed wire loop lying in a plane tilted TILT degrees from
# horizontal: a horizontal leg from the hub out to radius R, a quarter-circle
# arc of radius R climbing up in the tilted plane, and an inclined leg running
# straight back down into the hub centre.  Four lobes, rotated 90 deg apart.
# ---------------------------------------------------------------------------

# ---------------- driving dimensions (mm) ----------------
R = 100.0            # lobe radius (length of straight legs = arc radius)
TILT = 50.0          # tilt of each lobe plane from horizontal (deg)
WIRE_D = 2.0         # wire diameter
N_LOBES = 4          # cloverleaf lobes, 90 deg apart

HUB_SIDES = 12
BASE_R = 12.5        # circumradius of lower (base) plate
BASE_T = 2.2         # thickness of lower plate (centred on wire junction)
GAP = 3.0            # gap between lower plate and upper nut
TOP_R = 10.0         # circumradius of upper nut
TOP_T = 1.9          # thickness of upper nut

SEAM_ROT = 145.0     # angular position of the swept wire's seam line (deg)

VIEW = {"azimuth": 45, "elevation": 26}

r = WIRE_D / 2.0
t = math.radians(TILT)


def _lobe_frame():
    O = cq.Vector(0, 0, 0)
    u = cq.Vector(0, 1, 0)                               # horizontal leg dir
    v = cq.Vector(math.cos(t), 0, math.sin(t))           # inclined leg dir
    return O, u, v


def lobe_swept():
    """Whole lobe swept as one wire with mitred ('right') corners."""
    O, u, v = _lobe_frame()
    A = u * R                       # end of horizontal leg
    B = v * R                       # top of inclined leg
    M = (u + v).normalized() * R    # arc mid point
    P = u * (BASE_R * 0.6)          # wire starts hidden inside the base plate
    arc = cq.Edge.makeThreePointArc(A, M, B).toSplines()
    path = cq.Wire.assembleEdges([cq.Edge.makeLine(P, A), arc,
                                  cq.Edge.makeLine(B, O)])
    prof = cq.Wire.makeCircle(r, P, u)
    # orient the profile so the seam of the tube sits where it is least seen
    s0 = (prof.startPoint() - P).normalized()
    ang = math.degrees(math.atan2(s0.cross(v).dot(u), s0.dot(v)))
    prof = prof.rotate(P, P + u, ang + SEAM_ROT)
    solid = cq.Solid.sweep(prof, [], path, True, False, None, "right")
    expected = math.pi * r * r * ((R - BASE_R * 0.6) + R * math.pi / 2 + R)
    return solid, expected


def lobe_pieces():
    """Fallback: straight legs as cylinders, arc as a revolved tube."""
    O, u, v = _lobe_frame()
    n = u.cross(v)
    A = u * R
    B = v * R
    leg1 = cq.Solid.makeCylinder(r, R, O, u)
    leg2 = cq.Solid.makeCylinder(r, R, O, v)
    arc = cq.Solid.revolve(cq.Wire.makeCircle(r, A, v), [], 90.0, O, n)
    return (cq.Workplane("XY").add(leg1)
            .union(cq.Workplane("XY").add(leg2))
            .union(cq.Workplane("XY").add(arc))).val()


def base_lobe():
    try:
        solid, expected = lobe_swept()
        if solid.isValid() and abs(solid.Volume() - expected) < 0.03 * expected:
            return solid
    except Exception:
        pass
    return lobe_pieces()


# ---------------- hub: lower base plate + upper nut (12-sided prisms) -------
base = (cq.Workplane("XY").workplane(offset=-BASE_T / 2.0)
        .polygon(HUB_SIDES, 2 * BASE_R).extrude(BASE_T))
top = (cq.Workplane("XY").workplane(offset=BASE_T / 2.0 + GAP)
       .polygon(HUB_SIDES, 2 * TOP_R).extrude(TOP_T))

result = base.union(top)

# ---------------- four lobes, polar pattern about Z ----------------
lobe0 = base_lobe()
for k in range(N_LOBES):
    lk = lobe0.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1),
                      -360.0 / N_LOBES * k)
    result = result.union(cq.Workplane("XY").add(lk))
